import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
MODULE = 2.0            # gear module
TEETH = 60              # number of teeth
PRESSURE_ANGLE = 20.0   # degrees
ADDENDUM = 1.0 * MODULE
DEDENDUM = 1.05 * MODULE     # root circle depth below the pitch circle;
                             # a full-round root (tangent to both flanks and
                             # the root circle) joins neighbouring teeth
FACE_WIDTH = 12.0       # gear thickness (Z)
HOLE_W = 12.0           # rectangular bore, along X
HOLE_H = 7.2            # rectangular bore, along Y
FLANK_PTS = 4           # interpolation points per involute flank
ROOT_PTS = 3            # interior interpolation points on the root round

# ---------------- derived ----------------
rp = MODULE * TEETH / 2.0
rb = rp * math.cos(math.radians(PRESSURE_ANGLE))
ra = rp + ADDENDUM
rf = rp - DEDENDUM
pitch_ang = 2.0 * math.pi / TEETH
alpha_p = math.radians(PRESSURE_ANGLE)
half_tooth_p = math.pi / (2.0 * TEETH)


def inv(a):
    return math.tan(a) - a


def half_angle(r):
    """Half angular tooth thickness at radius r (involute flank)."""
    r = max(r, rb)
    a = math.acos(rb / r)
    return half_tooth_p + inv(alpha_p) - inv(a)


def pol(r, ang):
    return (r * math.cos(ang), r * math.sin(ang))


def flank_pt(center, side, r):
    return pol(r, center + side * half_angle(r))


def flank_tangent(center, side, r):
    """Unit tangent of the flank, pointing towards increasing radius."""
    dr = 1e-5
    p0 = flank_pt(center, side, r)
    p1 = flank_pt(center, side, r + dr)
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    n = math.hypot(dx, dy)
    return (dx / n, dy / n)


def root_round(r_s):
    """Centre distance and radius of the full-round root arc that is tangent
    to both flanks at r_s (centre on the gap bisector of the gap at +pitch/2)."""
    gap_c = pitch_ang / 2.0
    p = flank_pt(0.0, +1, r_s)
    t = flank_tangent(0.0, +1, r_s)
    nrm = (-t[1], t[0])
    u = (math.cos(gap_c), math.sin(gap_c))
    a11, a12, a21, a22 = nrm[0], -u[0], nrm[1], -u[1]
    det = a11 * a22 - a12 * a21
    R = (-p[0] * a22 + p[1] * a12) / det
    s = (-a11 * p[1] + a21 * p[0]) / det
    return s, R


# radius where the flank hands over to the root round, found so that the
# bottom of the round lies on the root circle
lo, hi = rb, rp
for _ in range(60):
    mid = 0.5 * (lo + hi)
    cc, RR = root_round(mid)
    if cc - RR < rf:
        lo = mid
    else:
        hi = mid
r_s = 0.5 * (lo + hi)
root_c, root_R = root_round(r_s)


def gap_points(c):
    """Points of the tooth gap between tooth at angle c and the next one:
    upper flank (tip -> r_s), root round, next lower flank (r_s -> tip)."""
    cn = c + pitch_ang
    gc = c + pitch_ang / 2.0
    rs_list = [ra + (r_s - ra) * k / (FLANK_PTS - 1) for k in range(FLANK_PTS)]
    pts = [flank_pt(c, +1, r) for r in rs_list]
    # root round: angles measured around its centre
    cx, cy = pol(root_c, gc)
    p0 = pts[-1]
    a0 = math.atan2(p0[1] - cy, p0[0] - cx)
    p1 = flank_pt(cn, -1, r_s)
    a1 = math.atan2(p1[1] - cy, p1[0] - cx)
    # sweep through the inner side (towards the gear centre)
    while a1 > a0:
        a1 -= 2.0 * math.pi
    for k in range(1, ROOT_PTS + 1):
        a = a0 + (a1 - a0) * k / (ROOT_PTS + 1)
        pts.append((cx + root_R * math.cos(a), cy + root_R * math.sin(a)))
    pts += [flank_pt(cn, -1, r) for r in rs_list[::-1]]
    return pts


# ---------------- tooth outline as one closed wire ----------------
wp = cq.Workplane("XY").moveTo(*flank_pt(0.0, +1, ra))
for i in range(TEETH):
    c = i * pitch_ang
    cn = c + pitch_ang
    pts = gap_points(c)
    t0 = flank_tangent(c, +1, ra)
    t1 = flank_tangent(cn, -1, ra)
    # one smooth edge per tooth gap (flank - root round - flank)
    wp = wp.spline(pts[1:], includeCurrent=True,
                   tangents=[(-t0[0], -t0[1]), t1])
    # flat top land on the tip circle
    if i < TEETH - 1:
        wp = wp.threePointArc(pol(ra, cn), flank_pt(cn, +1, ra))
    else:
        wp = wp.threePointArc(pol(ra, cn), flank_pt(0.0, +1, ra))

gear = wp.close().extrude(FACE_WIDTH)

# rectangular through bore
bore = (cq.Workplane("XY").workplane(offset=-1.0)
        .rect(HOLE_W, HOLE_H).extrude(FACE_WIDTH + 2.0))
result = gear.cut(bore)

VIEW = {"azimuth": 45, "elevation": 26}
